import math

import cadquery as cq

# =====================================================================
# Clamp / slide block: rectangular body with a 45 deg chamfered bottom,
# a raised rounded ridge on top (ramped down at the +X end), a deep
# counterbored through hole, shallow side panels, bottom corner notches
# and pockets, and mitred corner blocks (visible as joint lines).
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
L = 100.0          # length along X
W = 47.0           # width along Y
H_BODY = 58.5      # height of main body (shoulder level)
H_TOP = 69.0       # top of ridge
RIDGE_W = 30.0     # ridge width (Y)
RIDGE_BASE_FIL = 2.2   # concave fillet at ridge base
RIDGE_TOP_RND = 0.8    # round on the long ridge top edges
RAMP_X = 38.6      # X where the ridge top starts descending (+X end ramp)
RAMP_SIDE_FIL = 4.0    # rounds between ramp and ridge sides
RAMP_TOP_FIL = 2.5     # round between ridge top and ramp
BOT_CH = 12.0      # 45 deg chamfer on all bottom edges

HOLE_X = -9.5      # hole position along X (centred in Y)
CB_D = 27.0        # counterbore diameter
CB_DEPTH = 11.5    # counterbore depth from ridge top
CB_CH = 0.7        # chamfer at counterbore mouth
HOLE_D = 13.0      # through hole
HOLE_CH = 0.7      # chamfer on both ends of the through hole
SPOT_D = 29.0      # shallow spot face on the bottom
SPOT_DEPTH = 0.3

# mitred corner blocks (joint lines)
JOINT_END_Y = 8.2      # joint offset from the centre line on the end faces
JOINT_SIDE_X = 15.3    # joint offset from the ends on the side faces

# shallow side panels (front and back)
PANEL_X0 = -L / 2 + JOINT_SIDE_X
PANEL_X1 = L / 2 - JOINT_SIDE_X
PANEL_Z0, PANEL_Z1 = 22.7, 48.6
PANEL_DEPTH = 0.5

# shallow stepped facet on the +X corner blocks of the side faces
TAB_X0, TAB_X1 = 36.4, 47.2     # lower tongue extent (X)
TAB_Z_LOW = 36.1                # bottom of the tongue
TAB_Z = 48.6                    # bottom of the band
TAB_DEPTH = 0.15

# bottom corner notches on front/back faces
NA_X = 15.6        # -X end notch length (open to the -X end)
NA_Z = 21.8        # -X end notch height
NA_D = 5.5         # -X end notch depth (Y)
NA_R = 3.9         # inner vertical round of the -X end notch
NB_XC = 41.6       # +X end vertical round pocket: axis X
NB_R = 5.8         # pocket radius
NB_E = 2.6         # pocket axis inset from the side face
NB_Z0 = 9.5        # +X end pocket floor
NB_Z = 20.5        # +X end pocket top
NS_X0, NS_X1 = 43.0, 47.4   # narrow slot above the +X pocket
NS_Z = 28.0
NS_D = 3.4

# +X end face: two slightly set-back bands and a small circular relief
END_BAND_Z = 48.8      # top of the lower band / bottom of the upper band
END_BAND_Z2 = 35.7     # bottom of the middle band
END_BAND_D1 = 0.3      # set-back of the upper band
END_BAND_D2 = 0.15     # set-back of the middle band
END_TOP_LIP = 1.0      # narrow full-depth lip left along the top edge
ARC_D = 13.0
ARC_ZC = 44.6
ARC_DEPTH = 1.0
# -X end face: shallow tab recess
NEG_TAB_HW = 18.5      # half width (Y)
NEG_TAB_DEPTH = 0.15
# -X corner blocks: upper part of the side faces set back slightly
NEG_UP_Z = 36.1
NEG_UP_DEPTH = 0.15

X0 = -L / 2
X1 = L / 2
hw = RIDGE_W / 2


class Pick(cq.Selector):
    """Select objects with an arbitrary predicate."""

    def __init__(self, f):
        self.f = f

    def filter(self, objs):
        return [o for o in objs if self.f(o)]


def arc_pts(c, r, a0, a1):
    """mid and end point of a circular arc about c from angle a0 to a1"""
    am = (a0 + a1) / 2
    return ((c[0] + r * math.cos(am), c[1] + r * math.sin(am)),
            (c[0] + r * math.cos(a1), c[1] + r * math.sin(a1)))


# ---------------- main body ----------------
body = (cq.Workplane("XY")
        .box(L, W, H_BODY, centered=(True, True, False))
        .edges("<Z").chamfer(BOT_CH))

# ---------------- ridge with ramped, rounded +X end ----------------
ZB = H_BODY - 1.0                                   # ridge solids start inside the body
ang = math.atan2(H_TOP - H_BODY, X1 - RAMP_X)       # ramp angle
t = RAMP_TOP_FIL * math.tan(ang / 2)
c_rt = (RAMP_X - t, H_TOP - RAMP_TOP_FIL)
# side (XZ) profile: flat top, rounded knee, ramp down to the +X end
side_prof = (cq.Workplane("XZ")
             .moveTo(X0, ZB).lineTo(X0, H_TOP).lineTo(c_rt[0], H_TOP)
             .threePointArc(*arc_pts(c_rt, RAMP_TOP_FIL, math.pi / 2, ang))
             .lineTo(X1, H_BODY).lineTo(X1, ZB).close()
             .extrude(W, both=True))
# cross-section (YZ) with small rounds on the top long edges
rr = RIDGE_TOP_RND
cs = (cq.Workplane("YZ", origin=(X0 - 2, 0, 0))
      .moveTo(-hw, ZB).lineTo(-hw, H_TOP - rr)
      .threePointArc(*arc_pts((-hw + rr, H_TOP - rr), rr, math.pi, math.pi / 2))
      .lineTo(hw - rr, H_TOP)
      .threePointArc(*arc_pts((hw - rr, H_TOP - rr), rr, math.pi / 2, 0))
      .lineTo(hw, ZB).close()
      .extrude(L + 4))
# prism running down the ramp that rounds the ramp / side edges
d_ramp = cq.Vector(math.cos(ang), 0, -math.sin(ang))
pl_ramp = cq.Plane(origin=cq.Vector((RAMP_X + X1) / 2, 0, (H_TOP + H_BODY) / 2),
                   xDir=cq.Vector(0, 1, 0), normal=d_ramp)
rs = RAMP_SIDE_FIL
ramp_round = (cq.Workplane(pl_ramp)
              .moveTo(-hw, -300).lineTo(hw, -300).lineTo(hw, -rs)
              .threePointArc(*arc_pts((hw - rs, -rs), rs, 0, math.pi / 2))
              .lineTo(-hw + rs, 0)
              .threePointArc(*arc_pts((-hw + rs, -rs), rs, math.pi / 2, math.pi))
              .close()
              .extrude(200, both=True))
ridge = side_prof.intersect(cs).intersect(ramp_round)

part = body.union(ridge)
# concave blend where the ridge meets the shoulders
part = (part.edges(cq.selectors.BoxSelector((X0 - 1, -hw - 6, H_BODY - 0.01),
                                            (X1 + 1, hw + 6, H_BODY + 0.01)))
        .edges(Pick(lambda e: abs(e.Center().x) < X1 - 0.1 and abs(e.Center().y) > 1))
        .fillet(RIDGE_BASE_FIL))

# ---------------- counterbored through hole ----------------
cbore = (cq.Workplane("XY", origin=(HOLE_X, 0, H_TOP - CB_DEPTH))
         .circle(CB_D / 2).extrude(CB_DEPTH + 1))
cb_ch = (cq.Workplane("XY", origin=(HOLE_X, 0, H_TOP - CB_CH))
         .circle(CB_D / 2).workplane(offset=CB_CH + 0.01)
         .circle(CB_D / 2 + CB_CH + 0.01).loft())
thru = (cq.Workplane("XY", origin=(HOLE_X, 0, -1))
        .circle(HOLE_D / 2).extrude(H_TOP + 2))
spot = (cq.Workplane("XY", origin=(HOLE_X, 0, -1))
        .circle(SPOT_D / 2).extrude(1 + SPOT_DEPTH))
z_floor = H_TOP - CB_DEPTH
h_ch_top = (cq.Workplane("XY", origin=(HOLE_X, 0, z_floor - HOLE_CH))
            .circle(HOLE_D / 2).workplane(offset=HOLE_CH + 0.01)
            .circle(HOLE_D / 2 + HOLE_CH + 0.01).loft())
h_ch_bot = (cq.Workplane("XY", origin=(HOLE_X, 0, SPOT_DEPTH - 0.01))
            .circle(HOLE_D / 2 + HOLE_CH + 0.01).workplane(offset=HOLE_CH + 0.01)
            .circle(HOLE_D / 2).loft())
part = (part.cut(cbore).cut(cb_ch).cut(thru).cut(spot)
        .cut(h_ch_top).cut(h_ch_bot))

# ---------------- bottom corner notches / pockets (front & back) ----------------
for sgn in (-1, 1):
    yf = sgn * W / 2          # side face plane

    # -X end bottom notch with rounded inner corner
    ya = yf - sgn * NA_D      # back wall of notch
    na = (cq.Workplane("XY")
          .box(NA_X + 1, NA_D + 1, NA_Z + 1, centered=False)
          .translate((X0 - 1, min(ya, yf + sgn * 1), -1)))
    na = na.edges("|Z").edges(
        Pick(lambda e: abs(e.Center().x - (X0 + NA_X)) < 1e-3
             and abs(e.Center().y - ya) < 1e-3)).fillet(NA_R)
    part = part.cut(na)

    # +X end pocket (vertical round pocket breaking out of the side face)
    nb = (cq.Workplane("XY", origin=(NB_XC, yf - sgn * NB_E, NB_Z0))
          .circle(NB_R).extrude(NB_Z - NB_Z0))
    part = part.cut(nb)

    # narrow slot above it with a 45 deg top
    ys = yf - sgn * NS_D
    slot = (cq.Workplane("XZ")
            .polyline([(NS_X0, 0), (NS_X1, 0), (NS_X1, NS_Z + (NS_X1 - NS_X0)),
                       (NS_X0, NS_Z)]).close()
            .extrude(-(NS_D + 1))
            .translate((0, min(ys, yf + sgn * 1), 0)))
    part = part.cut(slot)

# ---------------- shallow cosmetic recesses (applied per block) ----------------
cosmetic = []        # applied to every block
cosmetic_px = []     # applied to the +X corner blocks only
cosmetic_nx = []     # applied to the -X corner blocks only
for sgn in (-1, 1):
    yf = sgn * W / 2
    # shallow side panel
    cosmetic.append(cq.Workplane("XY")
                    .box(PANEL_X1 - PANEL_X0, 2 * PANEL_DEPTH, PANEL_Z1 - PANEL_Z0,
                         centered=(False, True, False))
                    .translate((PANEL_X0, yf, PANEL_Z0)).val())
    # stepped facet on the +X corner block: band above TAB_Z with a tongue below
    tab = (cq.Workplane("XZ")
           .polyline([(X1 - 20, TAB_Z), (TAB_X0, TAB_Z), (TAB_X0, TAB_Z_LOW),
                      (TAB_X1, TAB_Z_LOW), (TAB_X1, TAB_Z), (X1 + 1, TAB_Z),
                      (X1 + 1, H_BODY + 1), (X1 - 20, H_BODY + 1)]).close()
           .extrude(TAB_DEPTH, both=True)
           .translate((0, yf, 0)))
    cosmetic_px.append(tab.val())
    # upper part of the -X corner block faces set back slightly
    cosmetic_nx.append(cq.Workplane("XY")
                       .box(21, 2 * NEG_UP_DEPTH, H_BODY + 1 - NEG_UP_Z,
                            centered=(False, True, False))
                       .translate((X0 - 1, yf, NEG_UP_Z)).val())
# +X end face: set-back bands and the small circular relief
for z0, z1, dep in ((END_BAND_Z, H_BODY - END_TOP_LIP, END_BAND_D1),
                    (END_BAND_Z2, END_BAND_Z, END_BAND_D2)):
    cosmetic.append(cq.Workplane("XY")
                    .box(dep + 1, W + 2, z1 - z0, centered=(False, True, False))
                    .translate((X1 - dep, 0, z0)).val())
arc = (cq.Workplane("YZ", origin=(X1 - END_BAND_D1 - ARC_DEPTH, 0, ARC_ZC))
       .circle(ARC_D / 2).extrude(ARC_DEPTH + 1))
arc_clip = (cq.Workplane("XY")
            .box(ARC_DEPTH + 2, ARC_D + 2, ARC_D, centered=(False, True, False))
            .translate((X1 - END_BAND_D1 - ARC_DEPTH - 0.5, 0, END_BAND_Z)))
cosmetic.append(arc.intersect(arc_clip).val())
# -X end face: shallow tab between the two band levels
cosmetic.append(cq.Workplane("XY")
                .box(NEG_TAB_DEPTH + 1, 2 * NEG_TAB_HW, END_BAND_Z - END_BAND_Z2,
                     centered=(False, True, False))
                .translate((X0 - 1, 0, END_BAND_Z2)).val())


# ---------------- mitred corner blocks ----------------
# The block is made of a core and four mitred corner blocks (45 deg in plan).
# Split the solid along those joint planes, apply the shallow recesses to each
# block and fuse the blocks back without merging coplanar faces, so the joint
# lines stay visible on the single resulting solid.
def joint_face(p0, p1, z0=-5.0, z1=H_TOP + 5.0, ext=3.0):
    (xa, ya_), (xb, yb) = p0, p1
    dx, dy = xb - xa, yb - ya_
    n = math.hypot(dx, dy)
    dx, dy = dx / n, dy / n
    a = (xa - dx * ext, ya_ - dy * ext)
    b = (xb + dx * ext, yb + dy * ext)
    w = cq.Wire.makePolygon([cq.Vector(a[0], a[1], z0), cq.Vector(b[0], b[1], z0),
                             cq.Vector(b[0], b[1], z1), cq.Vector(a[0], a[1], z1)],
                            close=True)
    return cq.Face.makeFromWires(w)


joints = []
for sy in (-1, 1):
    joints.append(joint_face((X0, sy * JOINT_END_Y), (X0 + JOINT_SIDE_X, sy * W / 2)))
    joints.append(joint_face((X1, sy * JOINT_END_Y), (X1 - JOINT_SIDE_X, sy * W / 2)))

whole = part.val()
blocks = []
for b in whole.split(*joints).Solids():
    xc = b.Center().x
    tools = list(cosmetic)
    if xc > X1 - JOINT_SIDE_X:
        tools += cosmetic_px
    elif xc < X0 + JOINT_SIDE_X:
        tools += cosmetic_nx
    blocks.append(b.cut(*tools))
joined = blocks[0].fuse(*blocks[1:]).Solids()
if (len(joined) == 1 and joined[0].isValid()
        and abs(joined[0].Volume() - whole.Volume()) < 0.02 * whole.Volume()):
    result = cq.Workplane("XY").add(joined[0])
else:   # fall back to the un-split solid
    result = cq.Workplane("XY").add(
        whole.cut(*(cosmetic + cosmetic_px + cosmetic_nx)).Solids()[0])
